import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------- base
R_FL = 50.0        # flange radius
T_FL = 4.5         # flange thickness
R_HOLE_FL = 44.5   # bolt circle radius of flange holes
D_HOLE_FL = 4.5
R_B = 41.3         # base housing radius
WALL = 3.0
Z_SEAM = 44.0      # top of housing body
Z_TOP = 47.8       # top of cap ring
Z_TT = 46.8        # top of turntable disc
Z_CEIL = 22.0      # underside of internal ceiling
Z_SIDE_HOLE = 13.0
D_SIDE_HOLE = 6.0

# ---------------------------------------------------------------- arm joints (Y, Z)
S = (11.8, 76.3)     # shoulder axis
E = (53.0, 168.0)    # elbow axis
W = (116.5, 253.0)   # wrist axis

# X extents of the members
BR_X = (-18.5, -2.0)     # shoulder bracket (servo housing)
UA_X = (-2.0, 16.8)      # upper arm (incl. hub cups)
FA_X = (-20.0, 1.5)      # forearm
WP_X = (1.5, 7.5)        # wrist plate

R_BR = 20.8          # bracket top radius around shoulder axis
BR_Y0 = -28.5
BR_ZV = 63.0         # height of vertical front edge of bracket

R_CUP = 18.0         # upper arm end radius around the hub cups
R_CUP_IN = 15.5      # hub cup recess radius
UA_WAIST = 24.0      # upper arm width at waist

FA_W = 25.0          # forearm width (in YZ plane)
FA_LEN = 117.0       # forearm length from elbow axis
R_FA_END = 17.0      # radius of the forearm lobe around the elbow

R_WP = 14.5          # wrist plate radius around the wrist axis
WP_NECK = (W[0] + 17.5, W[1] + 13.0)   # centre of the plate's neck towards the gripper
R_NECK = 9.0

# gripper
G_ANG = 29.0                     # tilt of gripper plane (deg)
G_ORIGIN = (-7.5, 151.0, 274.8)  # gear-centre midpoint on bottom of stack
GEAR_C = 14.0                    # half distance of gear centres
GEAR_R = 12.6                    # root disc radius
GEAR_TIP = 14.8                  # tooth tip radius
TOOTH_PITCH = 12.0               # deg between teeth
LAY = 4.0          # link layer thickness
GAP = 1.0          # washer gap between layers
FING = 9.0         # finger thickness


def yz_solid(sketch_fn, x0, x1):
    """Extrude a YZ-plane outline along +X from x0 to x1."""
    wp = cq.Workplane("YZ", origin=(x0, 0, 0))
    return sketch_fn(wp).extrude(x1 - x0)


def circle_yz(c, r, x0, x1):
    return yz_solid(lambda wp: wp.center(c[0], c[1]).circle(r), x0, x1)


def poly_yz(pts, x0, x1):
    return yz_solid(lambda wp: wp.polyline(pts).close(), x0, x1)


def rect_yz(c, ang, l, w, x0, x1):
    return (
        cq.Workplane("YZ", origin=(x0, c[0], c[1]))
        .transformed(rotate=(0, 0, ang))
        .rect(l, w)
        .extrude(x1 - x0)
    )


def tangent_pt(p, c, r, upper=True):
    """Tangent point on circle (c, r) of a line from external point p."""
    dx, dy = c[0] - p[0], c[1] - p[1]
    d = math.hypot(dx, dy)
    base = math.atan2(dy, dx)
    off = math.asin(r / d)
    ang = base + off if upper else base - off
    L = math.sqrt(d * d - r * r)
    return (p[0] + L * math.cos(ang), p[1] + L * math.sin(ang))


def hull2(c0, c1, r0, r1):
    """Outline points of the straight part of the hull of two circles."""
    dx, dy = c1[0] - c0[0], c1[1] - c0[1]
    L = math.hypot(dx, dy)
    ux, uy = dx / L, dy / L
    nx, ny = -uy, ux
    a = math.asin((r0 - r1) / L)
    ca, sa = math.cos(a), math.sin(a)
    n1 = (nx * ca + ux * sa, ny * ca + uy * sa)
    n2 = (-nx * ca + ux * sa, -ny * ca + uy * sa)
    return [
        (c0[0] + n1[0] * r0, c0[1] + n1[1] * r0),
        (c1[0] + n1[0] * r1, c1[1] + n1[1] * r1),
        (c1[0] + n2[0] * r1, c1[1] + n2[1] * r1),
        (c0[0] + n2[0] * r0, c0[1] + n2[1] * r0),
    ]


def stadium_yz(c0, c1, r0, r1, x0, x1):
    s = poly_yz(hull2(c0, c1, r0, r1), x0, x1)
    return s.union(circle_yz(c0, r0, x0, x1)).union(circle_yz(c1, r1, x0, x1))


def lerp(p, q, t):
    return (p[0] + (q[0] - p[0]) * t, p[1] + (q[1] - p[1]) * t)


# ================================================================ BASE
flange = cq.Workplane("XY").circle(R_FL).circle(R_B - WALL).extrude(T_FL)
flange = flange.cut(
    cq.Workplane("XY").polarArray(R_HOLE_FL, 45, 360, 4).circle(D_HOLE_FL / 2).extrude(T_FL)
)
housing = (
    cq.Workplane("XY", origin=(0, 0, T_FL)).circle(R_B).circle(R_B - WALL).extrude(Z_SEAM - T_FL)
)
ceiling = cq.Workplane("XY", origin=(0, 0, Z_CEIL)).circle(R_B - WALL).extrude(Z_SEAM - Z_CEIL)
cap = (
    cq.Workplane("XY", origin=(0, 0, Z_SEAM))
    .circle(R_B + 0.9).circle(R_B - 1.3).extrude(Z_TOP - Z_SEAM)
)
turntable = cq.Workplane("XY", origin=(0, 0, Z_SEAM)).circle(R_B - 1.8).extrude(Z_TT - Z_SEAM)
turntable = turntable.cut(
    cq.Workplane("XY", origin=(0, 0, Z_TT - 0.6)).circle(R_B - 3.5).circle(R_B - 4.3).extrude(1)
)
base = flange.union(housing).union(ceiling).union(cap).union(turntable)
# put the cylinder seams on the -X side where they are least visible
base = base.rotate((0, 0, 0), (0, 0, 1), 180)
# side cable hole on +X with counterbore
base = base.cut(cq.Workplane("YZ", origin=(R_B - 6, 0, Z_SIDE_HOLE)).circle(D_SIDE_HOLE / 2).extrude(10))
base = base.cut(
    cq.Workplane("YZ", origin=(R_B - 1.0, 0, Z_SIDE_HOLE)).circle(D_SIDE_HOLE / 2 + 1.2).extrude(3)
)
# base servo hanging below the ceiling and its mounting plate
base_servo = (
    cq.Workplane("XY", origin=(-15, -15, Z_CEIL)).transformed(rotate=(0, 0, 45)).rect(24, 20).extrude(-15)
)
servo_plate = (
    cq.Workplane("XY", origin=(12, 12, Z_CEIL - 4)).transformed(rotate=(0, 0, 45)).rect(42, 26).extrude(4.5)
)
servo_plate = servo_plate.cut(
    cq.Workplane("XY", origin=(14, 14, Z_CEIL - 5)).transformed(rotate=(0, 0, 45)).slot2D(24, 7).extrude(3)
)
base = base.union(base_servo).union(servo_plate.intersect(
    cq.Workplane("XY").circle(R_B - WALL).extrude(Z_SEAM)))

# ================================================================ SHOULDER BRACKET
def corner_fillet(p, q1, q2, rf):
    """Fillet of radius rf at corner p between rays p->q1 and p->q2: (start on ray1, mid, end on ray2)."""
    d1 = (q1[0] - p[0], q1[1] - p[1])
    d2 = (q2[0] - p[0], q2[1] - p[1])
    l1, l2 = math.hypot(*d1), math.hypot(*d2)
    d1 = (d1[0] / l1, d1[1] / l1)
    d2 = (d2[0] / l2, d2[1] / l2)
    th = math.acos(max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1])))
    t = rf / math.tan(th / 2)
    b = (d1[0] + d2[0], d1[1] + d2[1])
    lb = math.hypot(*b)
    b = (b[0] / lb, b[1] / lb)
    cdist = rf / math.sin(th / 2)
    mid = (p[0] + b[0] * (cdist - rf), p[1] + b[1] * (cdist - rf))
    return (p[0] + d1[0] * t, p[1] + d1[1] * t), mid, (p[0] + d2[0] * t, p[1] + d2[1] * t)


tp = tangent_pt((BR_Y0, BR_ZV), S, R_BR, upper=True)
BR_BACK = (22.3, 56.0)      # rear vertical edge of the bracket (Y, top Z)
tb = tangent_pt(BR_BACK, S, R_BR, upper=False)
f_a, f_m, f_b = corner_fillet((BR_Y0, BR_ZV), (BR_Y0, Z_TT), tp, 9.0)
a_tb = math.atan2(tb[1] - S[1], tb[0] - S[0])
a_tp = math.atan2(tp[1] - S[1], tp[0] - S[0])
top_ang = (a_tb + a_tp) / 2
top_mid = (S[0] + R_BR * math.cos(top_ang), S[1] + R_BR * math.sin(top_ang))


def br_outline(wp):
    return (
        wp.moveTo(BR_Y0, Z_TT)
        .lineTo(BR_BACK[0], Z_TT)
        .lineTo(*BR_BACK)
        .lineTo(*tb)
        .threePointArc(top_mid, tp)
        .lineTo(*f_b)
        .threePointArc(f_m, f_a)
        .close()
    )


BR_DRAFT = 0.066     # the -X face leans inward by this dX per mm of height
bracket = yz_solid(br_outline, *BR_X)
_dn = math.hypot(1.0, BR_DRAFT)
draft_cut = cq.Workplane(
    cq.Plane(origin=(BR_X[0], 0, Z_TT), xDir=(0, 1, 0), normal=(-1.0 / _dn, 0, BR_DRAFT / _dn))
).rect(300, 300).extrude(40)
bracket = bracket.cut(draft_cut)
try:
    bracket = bracket.faces(">X or <X").edges().fillet(1.5)
except Exception:
    pass
# servo pocket on -X face (frame + servo body inside)
pocket = rect_yz((S[0] - 2, S[1] - 4), 35, 26, 18, BR_X[0] - 1, BR_X[0] + 7)
bracket = bracket.cut(pocket)
bracket = bracket.union(rect_yz((S[0] - 2, S[1] - 4), 35, 22, 14, BR_X[0] + 3.5, BR_X[0] + 7))
# front cable clip with slot
clip = cq.Workplane("XY", origin=(8.0, -17.5, Z_TT)).rect(13, 5).extrude(8.5)
clip = clip.edges("|Y").fillet(2.0)
clip = clip.cut(cq.Workplane("XZ", origin=(8.0, -14, Z_TT + 4.5)).rect(7, 3).extrude(8))
# small hook near the hub
hook = cq.Workplane("XY", origin=(5.0, -6.0, 63.5)).rect(6, 7).extrude(6)
hook = hook.cut(cq.Workplane("YZ", origin=(0, -7.5, 66.5)).circle(1.6).extrude(10))
bracket = bracket.union(clip)

# ================================================================ UPPER ARM
ua_dir = (E[0] - S[0], E[1] - S[1])
ua_len = math.hypot(*ua_dir)
ua_ux, ua_uy = ua_dir[0] / ua_len, ua_dir[1] / ua_len
ua_nx, ua_ny = -ua_uy, ua_ux
ua_mid = lerp(S, E, 0.5)


def ua_outline(wp):
    r = R_CUP
    p1 = (S[0] + ua_nx * r, S[1] + ua_ny * r)
    p2 = (E[0] + ua_nx * r, E[1] + ua_ny * r)
    p3 = (E[0] - ua_nx * r, E[1] - ua_ny * r)
    p4 = (S[0] - ua_nx * r, S[1] - ua_ny * r)
    m1 = (ua_mid[0] + ua_nx * UA_WAIST / 2, ua_mid[1] + ua_ny * UA_WAIST / 2)
    m2 = (ua_mid[0] - ua_nx * UA_WAIST / 2, ua_mid[1] - ua_ny * UA_WAIST / 2)
    e_top = (E[0] + ua_ux * r, E[1] + ua_uy * r)
    s_bot = (S[0] - ua_ux * r, S[1] - ua_uy * r)
    return (
        wp.moveTo(*p1)
        .threePointArc(m1, p2)
        .threePointArc(e_top, p3)
        .threePointArc(m2, p4)
        .threePointArc(s_bot, p1)
        .close()
    )


UA_HUB_X = 8.5       # +X face of the hub ends (cups); the waist rises to UA_X[1]
UA_BEVEL_K = 0.34    # slope of the bevels between waist and hubs (dX per mm along the arm)
UA_BEVEL_S = (14.0, 88.0)   # where the bevels start, measured from the shoulder axis
ua_p3 = (0.0, -ua_uy, ua_ux)                 # in-plane normal of the arm (3D)


def ua_bevel_cutter(s1, sign):
    """Half-space X + sign*k*(s - s1) > UA_X[1] as a large box (s = distance from S along the arm)."""
    nx, na = 1.0, sign * UA_BEVEL_K
    ln = math.hypot(nx, na)
    normal = (nx / ln, na * ua_ux / ln, na * ua_uy / ln)
    origin = (UA_X[1], S[0] + ua_ux * s1, S[1] + ua_uy * s1)
    pl = cq.Plane(origin=origin, xDir=ua_p3, normal=normal)
    return cq.Workplane(pl).rect(300, 300).extrude(80)


ua_hub = yz_solid(ua_outline, UA_X[0], UA_HUB_X)
try:
    ua_hub = ua_hub.faces("<X").edges().fillet(2.5)
except Exception:
    pass
ua_body = yz_solid(ua_outline, UA_HUB_X - 1.0, UA_X[1])
ua_body = ua_body.cut(ua_bevel_cutter(UA_BEVEL_S[1], 1.0)).cut(ua_bevel_cutter(UA_BEVEL_S[0], -1.0))
try:
    ua_body = ua_body.faces(">X").edges().fillet(3.0)
except Exception:
    pass
ua = ua_hub.union(ua_body)
ua = ua.union(hook)
# hub cups on the +X side of both ends
for c in (S, E):
    ua = ua.cut(circle_yz(c, R_CUP_IN, UA_HUB_X - 5.0, UA_X[1] + 1))
    ua = ua.cut(circle_yz(c, 2.4, UA_HUB_X - 8, UA_HUB_X))
    for k in (-1, 1):
        off = (c[0] + k * 4.5 * math.cos(math.radians(60)), c[1] + k * 4.5 * math.sin(math.radians(60)))
        ua = ua.cut(circle_yz(off, 0.9, UA_HUB_X - 7, UA_HUB_X))

# ================================================================ FOREARM
fa_dir = (W[0] - E[0], W[1] - E[1])
fa_l = math.hypot(*fa_dir)
fa_u = (fa_dir[0] / fa_l, fa_dir[1] / fa_l)
fa_n = (-fa_u[1], fa_u[0])
fa_ang = math.degrees(math.atan2(fa_u[1], fa_u[0]))


def fa_pt(t, s=0.0):
    return (E[0] + fa_u[0] * t + fa_n[0] * s, E[1] + fa_u[1] * t + fa_n[1] * s)


FA_SPLIT = -12.0    # x where the -X side plate meets the +X servo box
FA_WRIST_C = 102.0  # centre of the wrist servo lobe (along the forearm)


def rrect_yz(c, ang, l, w, r, x0, x1):
    s = rect_yz(c, ang, l, w, x0, x1)
    return s.edges("|X").fillet(r)


# -X side plate: dog-bone with lobes around the two servos
fa_plate = circle_yz(E, R_FA_END, FA_X[0], FA_SPLIT)
fa_plate = fa_plate.union(rect_yz(fa_pt(FA_WRIST_C / 2), fa_ang, FA_WRIST_C, FA_W, FA_X[0], FA_SPLIT))
fa_plate = fa_plate.union(rrect_yz(fa_pt(FA_WRIST_C), fa_ang, 30.0, FA_W + 1.0, 9.0, FA_X[0], FA_SPLIT))
try:
    fa_plate = fa_plate.faces("<X").edges().fillet(3.0)
except Exception:
    pass
fa_core = circle_yz(E, 14.0, FA_SPLIT - 0.5, UA_X[0])
FA_BOX_T0 = R_CUP - 3.0
fa_box = rect_yz(fa_pt((FA_BOX_T0 + FA_LEN) / 2), fa_ang, FA_LEN - FA_BOX_T0, FA_W, FA_SPLIT, FA_X[1])
fa_axis_sel = cq.selectors.ParallelDirSelector(cq.Vector(0, fa_u[0], fa_u[1]))
try:
    fa_box = fa_box.edges(fa_axis_sel).fillet(2.5)
except Exception:
    pass
forearm = fa_plate.union(fa_core).union(fa_box)
# rounded middle band (wrist roll housing) on the +X half
band = rect_yz(fa_pt(53.5), fa_ang, 39.0, FA_W, -5.5, FA_X[1] + 0.8)
try:
    band = band.edges(fa_axis_sel).edges("<X").fillet(4.2)
    band = band.edges(fa_axis_sel).edges(">X").fillet(2.0)
except Exception:
    pass
forearm = forearm.union(band)
# transverse grooves
for t in (34.0, 73.0):
    ring = rect_yz(fa_pt(t), fa_ang, 0.8, FA_W + 6, -5.5, FA_X[1] + 2).cut(
        rect_yz(fa_pt(t), fa_ang, 2.0, FA_W - 1.6, -6.5, FA_X[1] - 0.8)
    )
    forearm = forearm.cut(ring)
# window on the upper (front) face between plate and band
win_c = fa_pt(53.5, FA_W / 2)
forearm = forearm.cut(rect_yz(win_c, fa_ang, 32, 12, -13.5, -5.0))
for t in (40.5, 66.5):
    forearm = forearm.union(rect_yz(fa_pt(t, FA_W / 2 - 3.75), fa_ang, 2.0, 5.5, -11.0, -7.5))
    forearm = forearm.union(
        rect_yz(fa_pt(t + (1.5 if t < 53.5 else -1.5), FA_W / 2 - 3.0), fa_ang, 1.2, 1.5, -14.0, -4.5)
    )
# servo pockets (frame + servo body) on the -X face at elbow and wrist
for (t, ang_off, l, w) in ((3.0, 5.0, 25.0, 19.0), (FA_WRIST_C, 0.0, 23.0, 18.0)):
    forearm = forearm.cut(rrect_yz(fa_pt(t), fa_ang + ang_off, l, w, 2.5, FA_X[0] - 1, FA_X[0] + 4))
    forearm = forearm.union(rect_yz(fa_pt(t), fa_ang + ang_off, l - 4, w - 4, FA_X[0] + 1.2, FA_X[0] + 4))
# elbow hub boss on -X face
forearm = forearm.union(circle_yz(E, 5.0, FA_X[0] + 0.5, FA_X[0] + 2.5))

# ================================================================ WRIST PLATE
wrist = stadium_yz(W, WP_NECK, R_WP, R_NECK, *WP_X)
try:
    wrist = wrist.faces(">X").edges().fillet(1.0)
except Exception:
    pass
wrist = wrist.cut(
    yz_solid(lambda wp: wp.center(W[0], W[1]).slot2D(10, 5, angle=25), WP_X[1] - 1.0, WP_X[1] + 1)
)
wrist = wrist.cut(circle_yz(W, 1.5, WP_X[0] - 1, WP_X[1] + 1))

# ================================================================ GRIPPER
ga = math.radians(G_ANG)
g_normal = (0.0, -math.sin(ga), math.cos(ga))


def gwp(w0=0.0):
    pl = cq.Plane(
        origin=(G_ORIGIN[0], G_ORIGIN[1] + g_normal[1] * w0, G_ORIGIN[2] + g_normal[2] * w0),
        xDir=(1, 0, 0),
        normal=g_normal,
    )
    return cq.Workplane(pl)


def g_bar(p0, p1, r, w0, h):
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    ang = math.degrees(math.atan2(dy, dx))
    cx, cy = (p0[0] + p1[0]) / 2, (p0[1] + p1[1]) / 2
    return gwp(w0).center(cx, cy).slot2D(L + 2 * r, 2 * r, angle=ang).extrude(h)


def sector_gear(c, face_ang, w0, h, phase, span=66.0):
    g = gwp(w0).center(*c).circle(GEAR_R).extrude(h)
    n = int(span // TOOTH_PITCH)
    for i in range(-n, n + 1):
        a = face_ang + phase + i * TOOTH_PITCH
        ra = math.radians(a)
        hw_root = math.radians(TOOTH_PITCH * 0.30)
        hw_tip = math.radians(TOOTH_PITCH * 0.14)
        r0, r1 = GEAR_R - 0.5, GEAR_TIP
        pts = [
            (c[0] + r0 * math.cos(ra - hw_root), c[1] + r0 * math.sin(ra - hw_root)),
            (c[0] + r1 * math.cos(ra - hw_tip), c[1] + r1 * math.sin(ra - hw_tip)),
            (c[0] + r1 * math.cos(ra + hw_tip), c[1] + r1 * math.sin(ra + hw_tip)),
            (c[0] + r0 * math.cos(ra + hw_root), c[1] + r0 * math.sin(ra + hw_root)),
        ]
        g = g.union(gwp(w0).polyline(pts).close().extrude(h))
    return g


# layout in gripper plane (u across, v along the fingers)
GL, GR = (-GEAR_C, 0.0), (GEAR_C, 0.0)
A_L, A_R = (-27.3, 28.6), (27.3, 28.6)
I_L, I_R = (-5.0, 19.7), (5.0, 19.7)
B_L, B_R = (-18.3, 49.0), (18.3, 49.0)

W_L1 = 0.0                  # lower link layer
W_F = W_L1 + LAY + GAP      # finger layer
W_L2 = W_F + FING + GAP     # upper link layer
W_TOP = W_L2 + LAY

parts = []
half_step = TOOTH_PITCH / 2.0
for w0 in (W_L1, W_L2):
    parts.append(sector_gear(GL, 0.0, w0, LAY, 0.0))
    parts.append(sector_gear(GR, 180.0, w0, LAY, half_step))
    for gc, a, i, b in ((GL, A_L, I_L, B_L), (GR, A_R, I_R, B_R)):
        parts.append(g_bar(gc, a, 5.2, w0, LAY))
        parts.append(g_bar(i, b, 4.0, w0, LAY))


def finger(sign):
    s = sign
    outer = [(s * 31.3, 34.0), (s * 29.9, 42.0), (s * 25.3, 61.5), (s * 22.3, 80.0), (s * 20.0, 88.5)]
    inner = [(s * 12.5, 77.7), (s * 11.9, 61.0), (s * 14.0, 53.0)]
    wp = gwp(W_F).moveTo(s * 21.5, 22.5)
    wp = wp.threePointArc((s * 29.0, 22.6), (s * 32.0, 28.5))
    wp = wp.spline(outer, includeCurrent=True)
    wp = wp.lineTo(s * 10.4, 88.5)
    wp = wp.spline(inner, includeCurrent=True)
    wp = wp.lineTo(s * 15.5, 42.0)
    wp = wp.close()
    return wp.extrude(FING)


parts.append(finger(-1))
parts.append(finger(1))
# pins through the stack
for p in (GL, GR, A_L, A_R, I_L, I_R, B_L, B_R):
    parts.append(gwp(W_L1 - 0.5).center(*p).circle(2.2).extrude(W_TOP + 1.0))
    for w0 in (W_L1 - 0.6, W_TOP):
        parts.append(gwp(w0).center(*p).circle(2.8).extrude(0.6))
# servo horn holes on left gear
horn_cut = (
    gwp(W_TOP - 1.0).center(GL[0] - 3.0, GL[1] + 2.0).circle(1.2).extrude(2)
    .union(gwp(W_TOP - 1.0).center(GL[0] + 1.0, GL[1] + 5.0).circle(1.0).extrude(2))
)
# gripper servo block under the left gear + connecting spine on wrist
servo_blk = gwp(-6.0).center(-10.0, 1.0).rect(35.0, 20.0).extrude(6.0)
spine = gwp(-8.0).center(14.5, -8.0).rect(10.0, 18.0).extrude(8.0)

gripper = parts[0]
for p in parts[1:]:
    gripper = gripper.union(p)
gripper = gripper.union(servo_blk).union(spine).cut(horn_cut)

# ================================================================ ASSEMBLE
result = (
    base.union(bracket)
    .union(ua)
    .union(forearm)
    .union(wrist)
    .union(gripper)
)
